"""Poke ball desk ornament: a ball (band groove around its equator, button on
top) sunk slightly into the back of a square plaque that carries an engraved
message on its front face and an engraved inscription on its top face.

Orientation: plaque at -Y with the message facing -Y, ball behind it (+Y),
button pointing up (+Z), band groove in a plane normal to Y.
"""
import cadquery as cq
from OCP.gp import gp_GTrsf, gp_Mat
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
R = 25.0                 # ball radius (ball centre at origin)
GROOVE_W = 3.55          # width of the equatorial band groove (along Y)
FEATURE_DY = -0.25       # band and button sit this far off the ball centre (Y)
GROOVE_D = 1.5           # shell thickness = depth of band groove and button opening
BTN_RECESS_R = 7.15      # radius of the shell opening around the button
BTN_OPENING_D = 1.6      # depth of that opening below the ball surface
BTN_RING_R = 5.7         # radius of the button ring (boss)
BTN_RING_TOP = 24.4      # top of the button ring
BTN_CAP_R = 4.3          # radius of the centre button cap
BTN_CAP_TOP = 25.1       # top of the centre button cap

PLAQUE_W = 2.008 * R     # square plaque side (X and Z)
PLAQUE_T = 10.0          # plaque thickness (Y)
PLAQUE_BACK_Y = -0.9 * R  # plaque back face, ball sinks slightly into it

TEXT_DEPTH = 0.5         # engraving depth
TEXT_MARGIN = 0.2        # text tools start this far outside the face
FRONT_CAP = 0.092        # cap height of the front message / plaque side
TOP_CAP = 0.483          # cap height of the top inscription / plaque thickness
TOP_BASE = 0.759         # top inscription baseline, from back face / thickness
CAP_RATIO = 0.729        # cap height / font size of the font used
FONT = "DejaVu Sans"

# ---------------- ball ----------------
# Built like a real poke ball: an outer shell of thickness GROOVE_D around a
# core sphere; the shell is split by the equatorial band gap and pierced by
# a round opening around the button, so both show the core surface.
# (Spheres and cylinders are turned so that their seam lines end up where
# they are cut away or hidden.)


def y_pole_sphere(radius, seam_up):
    """Sphere with its poles on the Y axis and its seam meridian passing
    through +Z (seam_up) or -Z."""
    return (
        cq.Workplane("XY")
        .sphere(radius)
        .rotate((0, 0, 0), (1, 0, 0), -90)
        .rotate((0, 0, 0), (0, 1, 0), -90 if seam_up else 90)
    )


def z_cylinder(radius, z0, z1, seam_deg):
    """Vertical cylinder on the button axis, seam turned to azimuth seam_deg."""
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .circle(radius)
        .extrude(z1 - z0)
        .rotate((0, 0, 0), (0, 0, 1), seam_deg)
        .translate((0, FEATURE_DY, 0))
    )


ball = cq.Workplane("XY").sphere(R)
core = y_pole_sphere(R - GROOVE_D, True)

# equatorial band gap (slab across the ball, normal to Y) minus the core
band = (
    cq.Workplane("XY")
    .box(3.0 * R, GROOVE_W, 3.0 * R)
    .translate((0, FEATURE_DY, 0))
    .cut(core)
)
ball = ball.cut(band)

# round opening in the shell around the button (on +Z), a touch deeper than
# the band so a small step edge marks its outline across the band floor
seat = y_pole_sphere(R - BTN_OPENING_D, False)
opening = z_cylinder(BTN_RECESS_R, 0.0, R + 5.0, 0).cut(seat)
ball = ball.cut(opening)

# button ring standing in the opening, and the centre cap on top of it
ring = z_cylinder(BTN_RING_R, R - BTN_OPENING_D - 1.5, BTN_RING_TOP, 45)
cap = z_cylinder(BTN_CAP_R, BTN_RING_TOP - 0.1, BTN_CAP_TOP, 45)
ball = ball.union(ring).union(cap)

# ---------------- plaque ----------------
front_y = PLAQUE_BACK_Y - PLAQUE_T
plaque = (
    cq.Workplane("XY")
    .box(PLAQUE_W, PLAQUE_T, PLAQUE_W)
    .translate((0, PLAQUE_BACK_Y - PLAQUE_T / 2.0, 0))
)

part = plaque.union(ball)

# ---------------- engraved text ----------------
def stretch_x(shape, sx):
    """Scale a shape along world X only (used to match the glyph widths)."""
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(sx, 0, 0, 0, 1, 0, 0, 0, 1))
    return cq.Shape.cast(BRepBuilderAPI_GTransform(shape.wrapped, g, True).Shape())


def text_tool(txt, plane, cap_h, u_left, u_right, kind):
    """Text solid with its baseline on the plane origin, cap height cap_h and
    its left/right extremes at u_left/u_right (fractions of the plaque width,
    measured from the -X edge).  Extruded 'into' the plane by TEXT_DEPTH and
    sticking out by a small margin so the cut is clean."""
    size = cap_h / CAP_RATIO
    t = (
        cq.Workplane(plane)
        .workplane(offset=TEXT_MARGIN)
        .text(txt, size, -(TEXT_DEPTH + TEXT_MARGIN), combine=False,
              font=FONT, kind=kind, halign="left", valign="bottom")
        .val()
    )
    bb = t.BoundingBox()
    sx = (u_right - u_left) * PLAQUE_W / (bb.xmax - bb.xmin)
    t = stretch_x(t, sx)
    x0 = -PLAQUE_W / 2.0 + u_left * PLAQUE_W - bb.xmin * sx
    return t.translate(cq.Vector(x0, 0, 0))


# front message: (text, left, right as fractions of the width, baseline as
# fraction of the height measured from the top edge)
LINES = [
    ("Never stop", 0.059, 0.726, 0.309),
    ("Catching 'em", 0.065, 0.9075, 0.484),
    ("Love,", 0.564, 0.886, 0.670),
    ("Dad", 0.564, 0.849, 0.847),
]
for txt, ul, ur, v in LINES:
    t = text_tool(txt, "XZ", FRONT_CAP * PLAQUE_W, ul, ur, "italic")
    t = t.translate(cq.Vector(0, front_y, PLAQUE_W / 2.0 - v * PLAQUE_W))
    part = part.cut(cq.Workplane("XY").add(t))

# top inscription, reading along +X with the letters standing towards +Y
tt = text_tool("UCSD ECE 2017", "XY", TOP_CAP * PLAQUE_T, 0.038, 0.959, "regular")
tt = tt.translate(cq.Vector(0, PLAQUE_BACK_Y - TOP_BASE * PLAQUE_T, PLAQUE_W / 2.0))
part = part.cut(cq.Workplane("XY").add(tt))

result = part
